"""Moulded protective cap / boot: a thin-walled shell, open underneath.

Tall back body with a rounded hood on top, a sloped front face with
cheeks, wide flared wings (flange) half way down with a front lip and
side skirts, a boss pad with a small hole on the inside of the back wall.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
Y_BACK = 46.0          # back face (+Y)
Y_TIP = -46.0          # front tips of the wings (-Y)
Y_FC = -41.8           # centre part of the chevron-shaped front edge
XH = 31.3              # half width of hood / back body
H = 65.8               # overall height
ZF = 37.7              # flange (wing) top
ZL = 26.9              # bottom of the front lip
ZS = 14.0              # bottom of the wing skirts
T = 2.0                # wall thickness

R_TOP = 9.0            # hood top edge round
R_VERT = 10.0          # back vertical edge round
R_TIP = 0.0            # vertical rounds on wing tips (sharp)
R_BEND = 6.0           # concave round at the chevron bend of the front edge
R_LIP = 2.5            # round on the flange top outer edge
CHEEK_BAND = 0.6       # depth of the chamfer band between sloped face and cheeks
R_JOIN = 2.5           # concave round between hood and flange top
R_JOIN_IN = 1.0        # matching round inside the shell

Y_SLOPE_TOP = -12.4    # sloped front face meets the top
Y_SLOPE_BOT = -38.5    # sloped front face meets the flange top
X_CH_F = 23.3          # half width of the sloped face at its foot
Y_CHEEK = -11.2        # cheek meets the hood side

# wing plan outline (+X half)
X_TIPW = 41.0          # x of the wing tip at the front
X_FC = 24.9            # chevron bend of the front edge
WING_BACK = [          # back edge of the wing, from the widest point
    (49.8, -3.7),      # to where it blends into the hood side
    (49.6, 0.1),
    (48.5, 3.4),
    (46.2, 5.9),
    (43.0, 7.6),
    (38.4, 8.9),
    (35.2, 10.5),
    (32.6, 13.7),
    (31.5, 17.6),
    (30.3, 22.0),
]

# bottom edge profile of the walls (side view)
Y_SKIRT_F = -17.8      # front edge of the skirt
R_SK = 3.4             # rounds on the skirt front edge
Y_SKIRT_B = 9.4        # skirt bottom ends, back body bottom rises
BOT_MID = (29.4, 6.8)  # a point on the curved bottom of the back body

# pad + hole on the back wall
PAD_HW = 10.8
PAD_H = 14.3
PAD_T = 1.8
HOLE_D = 2.4
HOLE_Z = 7.5

BIG = 200.0


# ---------------- helpers ----------------
class _FSel(cq.Selector):
    def __init__(self, f):
        self.f = f

    def filter(self, objs):
        return self.f(objs)


def _near(x, y, tol):
    return cq.selectors.BoxSelector((x - tol, y - tol, -BIG),
                                    (x + tol, y + tol, BIG))


def _junction(z, xmax, ymin):
    """concave edges where the hood sides / cheeks meet the flange top"""
    def f(objs):
        out = []
        for o in objs:
            bb = o.BoundingBox()
            if (abs(bb.zmin - z) < 0.05 and abs(bb.zmax - z) < 0.05
                    and max(abs(bb.xmin), abs(bb.xmax)) <= xmax
                    and bb.ymin > ymin and (bb.ymax - bb.ymin) > 3.0):
                out.append(o)
        return out
    return _FSel(f)


def _offset_pts(pts, off):
    """offset a CCW point loop inwards by `off` (mitred corners)"""
    n = len(pts)
    out = []
    for i in range(n):
        p, a, b = pts[i], pts[i - 1], pts[(i + 1) % n]
        d1 = (p[0] - a[0], p[1] - a[1])
        d2 = (b[0] - p[0], b[1] - p[1])
        l1, l2 = math.hypot(*d1), math.hypot(*d2)
        n1 = (-d1[1] / l1, d1[0] / l1)      # left normal = inward for CCW
        n2 = (-d2[1] / l2, d2[0] / l2)
        nx, ny = n1[0] + n2[0], n1[1] + n2[1]
        ln = math.hypot(nx, ny)
        nx, ny = nx / ln, ny / ln
        k = off / max(0.2, nx * n1[0] + ny * n1[1])
        out.append((p[0] + nx * k, p[1] + ny * k))
    return out


# ---------------- hood + back body ----------------
def upper_body(off):
    """hood + back body, offset inwards by `off` (0 = outer skin)"""
    xh = XH - off
    yb = Y_BACK - off
    yf = Y_FC - 10.0
    h = H - off
    zb = -10.0 if off > 0 else 0.0
    zcut = ZF - off - (0.5 if off > 0 else 0.0)
    u = (cq.Workplane("XY").workplane(offset=zb)
         .center(0, (yf + yb) / 2.0)
         .rect(2 * xh, yb - yf)
         .extrude(h - zb))
    u = u.edges("|Z and >Y").fillet(R_VERT - off)
    u = u.faces(">Z").edges("not <Y").fillet(R_TOP - off)

    # sloped front face (only above the flange top), shifted by `off`
    ang = math.atan2(H - ZF, Y_SLOPE_TOP - Y_SLOPE_BOT)
    ta = math.tan(ang)
    dy = off / math.sin(ang)
    y_at_z = Y_SLOPE_BOT + dy + (zcut - ZF) / ta
    y_top = Y_SLOPE_BOT + dy + (H + 20 - ZF) / ta
    slope_cut = (cq.Workplane("YZ")
                 .polyline([(y_at_z, zcut), (y_top, H + 20),
                            (-BIG, H + 20), (-BIG, zcut)])
                 .close()
                 .extrude(BIG / 2, both=True))
    u = u.cut(slope_cut)

    # cheeks: vertical planes from the slope foot to the hood side
    for s in (1, -1):
        ax, ay = s * X_CH_F, Y_SLOPE_BOT
        bx, by = s * XH, Y_CHEEK
        ln = math.hypot(bx - ax, by - ay)
        ux, uy = (bx - ax) / ln, (by - ay) / ln
        nx, ny = -uy * s, ux * s
        if nx * s > 0:
            nx, ny = -nx, -ny
        ax, ay = ax + nx * off, ay + ny * off
        bx, by = bx + nx * off, by + ny * off
        p0 = (ax - ux * 60, ay - uy * 60)
        p1 = (bx + ux * 20, by + uy * 20)
        pts = [p0, p1, (p1[0] - nx * 40, p1[1] - ny * 40),
               (p0[0] - nx * 40, p0[1] - ny * 40)]
        ck = (cq.Workplane("XY").workplane(offset=zcut)
              .polyline(pts).close().extrude(H + 10))
        u = u.cut(ck)

    # narrow chamfer band between the sloped face and each cheek
    if CHEEK_BAND > 0:
        ns = (0.0, -math.sin(ang), math.cos(ang))
        for s in (1, -1):
            ex, ey = s * (XH - X_CH_F), Y_CHEEK - Y_SLOPE_BOT
            el = math.hypot(ex, ey)
            nc = (s * ey / el, -abs(ex) / el, 0.0)
            nx, ny, nz = ns[0] + nc[0], ns[1] + nc[1], ns[2] + nc[2]
            nl = math.sqrt(nx * nx + ny * ny + nz * nz)
            n = (nx / nl, ny / nl, nz / nl)
            a = (s * X_CH_F, Y_SLOPE_BOT, ZF)
            d = CHEEK_BAND + off
            org = (a[0] - n[0] * d, a[1] - n[1] * d, a[2] - n[2] * d)
            e3 = (ex, ey, ey * ta)
            e3l = math.sqrt(sum(c * c for c in e3))
            e3 = tuple(c / e3l for c in e3)
            pl = cq.Plane(origin=org, xDir=e3, normal=n)
            band = cq.Workplane(pl).rect(300, 300).extrude(100)
            band = band.intersect(cq.Workplane("XY").workplane(offset=zcut)
                                  .rect(BIG, BIG).extrude(H + 20))
            u = u.cut(band)

    # the wing block provides the front-lower part
    u = u.cut(cq.Workplane("XY").workplane(offset=-20)
              .center(0, -BIG / 2 - 38.0 + 2.5 * off)
              .rect(BIG, BIG).extrude(zcut + 20))
    return u


# ---------------- wings / flange ----------------
def wing_block(off):
    zb = -10.0 if off > 0 else 0.0
    right = [(X_FC, Y_FC), (X_TIPW, Y_TIP)] + WING_BACK
    nr = len(right)
    left = [(-x, y) for x, y in reversed(right)]
    pts = right + left
    if off > 0:
        pts = _offset_pts(pts, off)
        # keep the junction points well inside the (inner) hood side
        for k in (nr - 1, nr):
            x, y = pts[k]
            pts[k] = (math.copysign(XH - off - 1.0, x), y)
    # tangent of the outer wing edge at the start of the back curve
    tx, ty = WING_BACK[0][0] - X_TIPW, WING_BACK[0][1] - Y_TIP
    tl = math.hypot(tx, ty)
    tx, ty = tx / tl, ty / tl
    wp = (cq.Workplane("XY").workplane(offset=zb)
          .moveTo(*pts[0]).lineTo(*pts[1]).lineTo(*pts[2])
          .spline(pts[3:nr], tangents=[(tx, ty), (-0.25, 1.0)],
                  includeCurrent=True)
          .lineTo(*pts[nr])
          .spline(pts[nr + 1:2 * nr - 2], tangents=[(-0.25, -1.0), (tx, -ty)],
                  includeCurrent=True)
          .lineTo(*pts[2 * nr - 2])
          .lineTo(*pts[2 * nr - 1])
          .close())
    blk = wp.extrude(ZF - off - zb)
    # vertical edge rounds: (x, y, radius of the outer skin, convex?)
    for cx, cy, r, convex in ((X_TIPW, Y_TIP, R_TIP, True),
                              (X_FC, Y_FC, R_BEND, False)):
        rr = r - off if convex else r + off
        if r <= 0 or rr < 0.3:
            continue
        for s in (1, -1):
            blk = blk.edges("|Z").edges(_near(s * cx, cy, 4.0)).fillet(rr)
    # rounded top outer edge of the flange
    if off == 0:
        blk = blk.faces(">Z").edges().fillet(R_LIP)
    return blk


# ---------------- outer skin and cavity ----------------
outer = upper_body(0.0).union(wing_block(0.0))
outer = outer.edges(_junction(ZF, XH + 0.6, Y_FC + R_LIP + 0.1)).fillet(R_JOIN)

inner = upper_body(T).union(wing_block(T), clean=False)
try:
    inner_f = (inner.edges(_junction(ZF - T, XH - T + 0.6, Y_FC + T + 0.1))
               .fillet(R_JOIN_IN))
    if inner_f.val().isValid():
        inner = inner_f
except Exception:
    pass

body = outer.cut(inner)

# ---------------- bottom edge profile of the walls ----------------
c1 = (Y_SKIRT_F - R_SK, ZL - R_SK)   # centre of concave round
c2 = (Y_SKIRT_F + R_SK, ZS + R_SK)   # centre of convex round
k = math.sqrt(0.5)
prof = (cq.Workplane("YZ")
        .moveTo(-BIG, -20)
        .lineTo(-BIG, ZL)
        .lineTo(Y_SKIRT_F - R_SK, ZL)
        .threePointArc((c1[0] + k * R_SK, c1[1] + k * R_SK),
                       (Y_SKIRT_F, ZL - R_SK))
        .lineTo(Y_SKIRT_F, ZS + R_SK)
        .threePointArc((c2[0] - k * R_SK, c2[1] - k * R_SK),
                       (Y_SKIRT_F + R_SK, ZS))
        .lineTo(Y_SKIRT_B, ZS)
        .threePointArc(BOT_MID, (Y_BACK + 0.01, 0.0))
        .lineTo(BIG, 0.0)
        .lineTo(BIG, -20)
        .close()
        .extrude(BIG / 2, both=True))
body = body.cut(prof)

# boss pad on the inside of the back wall (its flat bottom sits at Z = 0,
# just below the rising bottom edge of the side walls)
pad = (cq.Workplane("XY")
       .center(0, Y_BACK - T - PAD_T / 2 + 0.25)
       .rect(2 * PAD_HW, PAD_T + 0.5)
       .extrude(PAD_H))
body = body.union(pad)

# small hole through the pad and the back wall
hole = (cq.Workplane("XZ", origin=(0, Y_BACK + 5, 0))
        .center(0, HOLE_Z).circle(HOLE_D / 2).extrude(T + PAD_T + 10))
body = body.cut(hole)

result = body
